"""Toy / game-pad shaped shell: a central dome with a flat top panel (screen
window, LED hole, four buttons), two side pods with horns at the back,
icosahedral knobs at the front and heart bosses on the flanks, all split by a
parting-line groove -- plus a separate small open-bottom box.

All organic lobes are scaled spheres (half ellipsoids); every size is driven
by the parameters below (mm)."""
import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
H_TOP = 53.5          # overall height (flat top cut plane), body bottom at Z=0
Z_SEAM = 25.4         # parting line height (widest section of all lobes)

# central body: two half-ellipsoids joined at the parting line
CB_AX, CB_AY = 48.7, 38.5
CB_CUP, CB_CLOW = 45.0, 20.4

# side pods: lower half-ellipsoid + inward-leaning crown
POD_AX, POD_AY = 16.6, 53.5
POD_CLOW = 25.4
POD_CROWN_H = 30.6    # crown height above the parting line
POD_CROWN_B = 53.2    # crown half length
POD_CROWN_K = 0.04    # inward lean of the crown centre per unit height
POD_CX, POD_CY = 49.2, 14.0
POD_ROT = 7.0         # splay angle (deg) about Z, backs turned outwards

# bridge between each pod crown and the top panel (centre X, centre Y, half axes)
BRIDGE_X, BRIDGE_Y = 39.2, 6.0
BRIDGE_A, BRIDGE_B, BRIDGE_C = 2.5, 13.0, 10.0

# horns at the back of the pods (elliptical cones, pod-local coordinates)
SPIKE_Z = 34.6                     # height of the horn tip
SPIKE_KZ, SPIKE_KX = 0.45, 0.36    # cone slope (radius/length) vertical / lateral
SPIKE_Y0, SPIKE_Y1 = 40.0, 62.0    # local pod Y of cone base / tip
SPIKE_TILT = 7.0                   # horn axis rises towards the tip (deg)
SPIKE_DX = 1.7                     # horn axis shifted towards the body centre

# icosahedral knobs at the pod fronts
KNOB_R = 6.5
KNOB_X, KNOB_YFRONT, KNOB_Z = 43.5, -42.3, 17.7

# heart bosses on the pod flanks
HEART_LOCAL_Y = 7.4
HEART_Z = 10.5
HEART_SIZE = 10.0
HEART_PROUD = 3.9

# parting-line groove
GROOVE_W = 0.7
GROOVE_D = 0.6

# top panel features
WIN_C = (-13.1, 7.5)                      # screen window (rectangular pocket)
WIN_W, WIN_L, WIN_D = 26.9, 22.9, 9.0
WIN_SLOT_W, WIN_SLOT_D = 3.0, 2.0         # undercut slot at the back edge of the window floor
LED_C = (-10.4, -16.3)
LED_D, LED_DEPTH = 6.8, 3.0
BTN_C = (23.5, -4.25)                     # four buttons in a diamond
BTN_OFF, BTN_D, BTN_DEPTH = 6.4, 6.0, 3.0

# front face features
FRONT_SLOT_X = (8.8, 22.6)
FRONT_SLOT_Z = (28.6, 32.6)
FRONT_SLOT_DEPTH = 2.0
FRONT_HOLE_X, FRONT_HOLE_Z, FRONT_HOLE_D = -22.2, 28.3, 7.0

# separate small box (open bottom)
BOX_C = (39.35, 181.3)
BOX_W, BOX_L, BOX_H = 23.5, 27.35, 13.3
BOX_Z0 = 4.5
BOX_WALL, BOX_TOP_T = 1.2, 1.5
BOX_HOLE_D = 17.2
BOX_PIN_D, BOX_PIN_INSET = 1.1, 1.9
BOX_BOSS_D = 3.2
BOX_SIDE_HOLE_DX, BOX_SIDE_HOLE_DZ = 6.6, 2.0
BOX_SLOT_L, BOX_SLOT_H, BOX_SLOT_Z = 9.0, 2.6, 4.0


# ---------------------------------------------------------------- helpers
def _scaled(shape, ax, ay, c):
    m = cq.Matrix([[ax, 0, 0, 0], [0, ay, 0, 0], [0, 0, c, 0], [0, 0, 0, 1]])
    return shape.transformGeometry(m)


def half_ellipsoid(ax, ay, c, upper=True, poles="y"):
    """Half ellipsoid standing on (upper) or hanging from (lower) the XY plane.
    Built from a 180 deg sphere wedge whose poles lie on the X or Y axis, so
    the curved face has no seam line running across it."""
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90, angleDegrees3=180)
    if poles == "x":
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
    s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90 if upper else -90)
    return _scaled(s, ax, ay, c)


def crown_axes(w0, h, k):
    """Cross-section ellipse with half-width w0 at z=0, crown height h and a
    crown centre drifting by k*z towards +x.  Returns the semi-axes (a, c) and
    the roll angle (deg) of the equivalent ellipse rolled about Y."""
    A = 1.0 / w0 ** 2
    B = -k * A
    C = 1.0 / h ** 2 + B * B / A
    tr, det = A + C, A * C - B * B
    d = math.sqrt(tr * tr / 4.0 - det)
    l_small, l_big = tr / 2.0 - d, tr / 2.0 + d
    c_ax, a_ax = 1.0 / math.sqrt(l_small), 1.0 / math.sqrt(l_big)
    vx, vz = B, l_small - A            # direction of the long (c) axis
    if vz < 0:
        vx, vz = -vx, -vz
    return a_ax, c_ax, math.degrees(math.atan2(vx, vz))


CROWN_DROP = 0.8      # crown ellipsoid centre sits this far below the parting plane
CROWN_POLES_Y = False


def crown(ax, ay, c, roll_deg, seam_deg=0.0):
    """Ellipsoid rolled about its long (Y) axis (positive roll leans the top to
    +X), centred CROWN_DROP below z=0 and kept above z=-0.2 so that it overlaps
    the lower half cleanly.  Poles on Y, sphere seam turned to the bottom."""
    if CROWN_POLES_Y:
        s = cq.Solid.makeSphere(1.0, pnt=cq.Vector(0, 0, 0), dir=cq.Vector(0, 1, 0),
                                angleDegrees1=-90, angleDegrees2=90, angleDegrees3=360)
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 180)
    else:
        s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_deg)
    s = _scaled(s, ax, ay, c)
    s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), roll_deg)
    s = s.translate(cq.Vector(0, 0, -CROWN_DROP))
    keep = cq.Solid.makeBox(4 * ay, 4 * ay, 4 * ay, pnt=cq.Vector(-2 * ay, -2 * ay, -0.2))
    return s.intersect(keep)


def pod_lobe(side, shrink=0.0):
    """One side pod in its local frame (parting plane at z=0, long axis Y)."""
    lo = half_ellipsoid(POD_AX - shrink, POD_AY - shrink, POD_CLOW - shrink, False, "y")
    # crown kept a hair inside the lower half at the parting plane (lost in the groove)
    a_u, c_u, roll = crown_axes(POD_AX - shrink - 0.2, POD_CROWN_H + CROWN_DROP - shrink,
                                POD_CROWN_K)
    up = crown(a_u, POD_CROWN_B - shrink, c_u, -side * roll, 0.0 if side < 0 else 180.0)
    return cq.Workplane("XY").add(up).union(cq.Workplane("XY").add(lo))


def centre_lobe(shrink=0.0):
    up = half_ellipsoid(CB_AX - shrink, CB_AY - shrink, CB_CUP - shrink, True, "x")
    lo = half_ellipsoid(CB_AX - shrink, CB_AY - shrink, CB_CLOW - shrink, False, "x")
    return cq.Workplane("XY").add(up).union(cq.Workplane("XY").add(lo))


def place_pod(shape_wp, side):
    return (shape_wp.rotate((0, 0, 0), (0, 0, 1), -side * POD_ROT)
            .translate((side * POD_CX, POD_CY, 0)))


def icosahedron(r):
    """Icosahedron with a vertex pointing to -Y and one ring vertex up (+Z)."""
    k = 1.0 / math.sqrt(5.0)
    rr = 2.0 * r * k
    front = cq.Vector(0, -r, 0)
    back = cq.Vector(0, r, 0)
    ring1 = [cq.Vector(rr * math.sin(math.radians(72 * i)), -r * k,
                       rr * math.cos(math.radians(72 * i))) for i in range(5)]
    ring2 = [cq.Vector(rr * math.sin(math.radians(72 * i + 36)), r * k,
                       rr * math.cos(math.radians(72 * i + 36))) for i in range(5)]
    tris = []
    for i in range(5):
        j = (i + 1) % 5
        tris.append((front, ring1[j], ring1[i]))
        tris.append((ring1[i], ring1[j], ring2[i]))
        tris.append((ring2[i], ring1[j], ring2[j]))
        tris.append((back, ring2[i], ring2[j]))
    faces = [cq.Face.makeFromWires(cq.Wire.makePolygon(list(t), close=True)) for t in tris]
    so = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
    if so.Volume() < 0:
        so = cq.Solid(so.wrapped.Reversed())
    return so


def heart_solid(size, thick):
    """Heart prism in the XY plane (tip towards +X), extruded along +Z."""
    r = 0.27 * size
    cu = -0.2 * size
    cv = 0.24 * size
    tip = 0.52 * size
    lob1 = cq.Workplane("XY").center(cu, cv).circle(r).extrude(thick)
    lob2 = cq.Workplane("XY").center(cu, -cv).circle(r).extrude(thick)
    a = math.radians(60)
    tri = (cq.Workplane("XY")
           .polyline([(cu + r * math.cos(a), cv + r * math.sin(a)), (tip, 0.0),
                      (cu + r * math.cos(a), -cv - r * math.sin(a)), (cu, 0.0)])
           .close().extrude(thick))
    return lob1.union(lob2).union(tri).val()


def body_lobes(shrink=0.0):
    res = centre_lobe(shrink).translate((0, 0, Z_SEAM))
    for side in (-1, 1):
        res = res.union(place_pod(pod_lobe(side, shrink).translate((0, 0, Z_SEAM)), side))
    return res


# ---------------------------------------------------------------- main body
body = body_lobes()

# bridges: hanging half-ellipsoids under the top plane blending the pod crowns into the panel
for side in (-1, 1):
    br = half_ellipsoid(BRIDGE_A, BRIDGE_B, BRIDGE_C, False, "y")
    body = body.union(cq.Workplane("XY").add(br).translate((side * BRIDGE_X, BRIDGE_Y, H_TOP)))

# flat top cut
body = body.intersect(cq.Workplane("XY").box(400, 400, H_TOP + 5, centered=(True, True, False))
                      .translate((0, 0, -5)))

# parting-line groove: thin slab outside a slightly shrunken copy of the lobes
inner = body_lobes(GROOVE_D)
slab = cq.Workplane("XY").box(400, 400, GROOVE_W).translate((0, 0, Z_SEAM))
body = body.cut(slab.cut(inner))

# horns
spike_len = SPIKE_Y1 - SPIKE_Y0
t = math.radians(SPIKE_TILT)
for side in (-1, 1):
    cone = cq.Solid.makeCone(SPIKE_KZ * spike_len, 0.0, spike_len,
                             pnt=cq.Vector(0, 0, 0), dir=cq.Vector(0, 1, 0))
    cone = cone.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 180)   # seam line underneath
    cone = _scaled(cone, SPIKE_KX / SPIKE_KZ, 1.0, 1.0)
    cw = (cq.Workplane("XY").add(cone)
          .rotate((0, 0, 0), (1, 0, 0), SPIKE_TILT)
          .translate((-side * SPIKE_DX, SPIKE_Y1 - spike_len * math.cos(t),
                      SPIKE_Z - spike_len * math.sin(t))))
    body = body.union(place_pod(cw, side))

# icosahedral knobs
for side in (-1, 1):
    ico = icosahedron(KNOB_R)
    ico = ico.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -side * POD_ROT)
    ico = ico.translate(cq.Vector(side * KNOB_X, KNOB_YFRONT + KNOB_R, KNOB_Z))
    body = body.union(cq.Workplane("XY").add(ico))

# heart bosses on the flanks, seated normal to the pod surface
for side in (-1, 1):
    dy = HEART_LOCAL_Y
    dz = HEART_Z - Z_SEAM
    xs = POD_AX * math.sqrt(max(1.0 - (dy / POD_AY) ** 2 - (dz / POD_CLOW) ** 2, 0.05))
    n = cq.Vector(xs / POD_AX ** 2, dy / POD_AY ** 2, dz / POD_CLOW ** 2).normalized()
    depth_in = 3.0
    hs = heart_solid(HEART_SIZE, depth_in + HEART_PROUD).translate(cq.Vector(0, 0, -depth_in))
    u = (cq.Vector(0, 1, 0) - n * n.y).normalized()      # heart tip points backwards
    hs = hs.moved(cq.Location(cq.Plane(origin=(xs, dy, dz), xDir=u, normal=n)))
    if side < 0:
        hs = hs.mirror("YZ")
    hs = hs.translate(cq.Vector(0, 0, Z_SEAM))
    body = body.union(place_pod(cq.Workplane("XY").add(hs), side))

# top panel: screen window with a floor slot, LED hole, diamond of buttons
win = (cq.Workplane("XY").box(WIN_W, WIN_L, WIN_D + 1, centered=(True, True, False))
       .translate((WIN_C[0], WIN_C[1], H_TOP - WIN_D)))
body = body.cut(win)
# undercut slot along the foot of the back wall of the window (hidden from above)
wslot = (cq.Workplane("XY").box(WIN_W, WIN_SLOT_W + 0.5, WIN_SLOT_D, centered=(True, False, False))
         .translate((WIN_C[0], WIN_C[1] + WIN_L / 2 - 0.5, H_TOP - WIN_D)))
body = body.cut(wslot)
led = (cq.Workplane("XY").circle(LED_D / 2).extrude(LED_DEPTH + 1)
       .translate((LED_C[0], LED_C[1], H_TOP - LED_DEPTH)))
body = body.cut(led)
for dx, dy in ((0, BTN_OFF), (0, -BTN_OFF), (BTN_OFF, 0), (-BTN_OFF, 0)):
    b = (cq.Workplane("XY").circle(BTN_D / 2).extrude(BTN_DEPTH + 1)
         .translate((BTN_C[0] + dx, BTN_C[1] + dy, H_TOP - BTN_DEPTH)))
    body = body.cut(b)


def front_y(x, z):
    """Y of the central body's front surface at (x, z)."""
    dz = z - Z_SEAM
    c = CB_CUP if dz >= 0 else CB_CLOW
    return -CB_AY * math.sqrt(max(1.0 - (x / CB_AX) ** 2 - (dz / c) ** 2, 0.0))


# front: rectangular slot and round hole on the parting line
sx = 0.5 * (FRONT_SLOT_X[0] + FRONT_SLOT_X[1])
sz = 0.5 * (FRONT_SLOT_Z[0] + FRONT_SLOT_Z[1])
slot = (cq.Workplane("XY").box(FRONT_SLOT_X[1] - FRONT_SLOT_X[0], 12.0,
                                 FRONT_SLOT_Z[1] - FRONT_SLOT_Z[0])
        .translate((sx, front_y(sx, sz) + FRONT_SLOT_DEPTH - 6.0, sz)))
body = body.cut(slot)
fh = (cq.Workplane("XZ").circle(FRONT_HOLE_D / 2).extrude(-12.0)
      .translate((FRONT_HOLE_X, front_y(FRONT_HOLE_X, FRONT_HOLE_Z) + 3.0 - 12.0, FRONT_HOLE_Z)))
body = body.cut(fh)

# ---------------------------------------------------------------- small box
box = cq.Workplane("XY").box(BOX_W, BOX_L, BOX_H, centered=(True, True, False))
box = box.cut(cq.Workplane("XY").box(BOX_W - 2 * BOX_WALL, BOX_L - 2 * BOX_WALL,
                                     BOX_H - BOX_TOP_T, centered=(True, True, False))
              .translate((0, 0, -0.01)))
# screw bosses in the corners under the lid
px, py = BOX_W / 2 - BOX_PIN_INSET, BOX_L / 2 - BOX_PIN_INSET
for sx_, sy_ in ((1, 1), (1, -1), (-1, 1), (-1, -1)):
    boss = (cq.Workplane("XY").circle(BOX_BOSS_D / 2).extrude(BOX_H * 0.5)
            .translate((sx_ * px, sy_ * py, BOX_H * 0.5 - 0.01)))
    box = box.union(boss)
box = box.faces(">Z").workplane().hole(BOX_HOLE_D)
box = (box.faces(">Z").workplane()
       .rect(2 * px, 2 * py, forConstruction=True)
       .vertices().hole(BOX_PIN_D, BOX_H * 0.5 + 1))
for sgn in (-1, 1):
    for dx in (-BOX_SIDE_HOLE_DX, BOX_SIDE_HOLE_DX):
        h = (cq.Workplane("XZ").circle(BOX_PIN_D / 2).extrude(-BOX_WALL * 3, both=True)
             .translate((dx, sgn * BOX_L / 2, BOX_H - BOX_SIDE_HOLE_DZ)))
        box = box.cut(h)
bslot = (cq.Workplane("XZ").slot2D(BOX_SLOT_L, BOX_SLOT_H).extrude(BOX_WALL * 3, both=True)
         .translate((0, BOX_L / 2, BOX_SLOT_Z)))
box = box.cut(bslot)
box = box.translate((BOX_C[0], BOX_C[1], BOX_Z0))

result = body.union(box)
